import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Inclined mounting bracket: a flat plate tilted about X, with a tall
# rounded-triangle mounting block on top, a small boss near the front edge,
# a horizontal lug at the bottom-left and an ear at the bottom-right.
# ---------------------------------------------------------------------------

# --- plate (local coords: u along X, v up the slope, z normal) -------------
THETA = 50.0          # plate inclination from horizontal [deg]
W = 100.0             # plate width (X)
L = 98.0              # plate length along the slope
T = 7.0               # plate thickness
R_CORNER = 6.5        # outer corner radius
EDGE_CH = 0.9         # small chamfer on plate perimeter edges

# ear at bottom-right
EAR_C = (106.5, 14.4)  # ear hole centre (u, v)
EAR_R = 6.4            # ear end radius
EAR_FOOT_U = 95.3      # where the slanted ear edge meets the front edge
EAR_NECK_V = 18.0      # where the upper ear edge leaves the plate side
EAR_FILLET = 1.0       # concave fillet between plate side and ear
EAR_HOLE_D = 6.2

# window
WIN_U = (12.5, 86.5)
WIN_V = (9.9, 48.6)
WIN_R = 5.5
WIN_CH = 1.0

# mounting holes in the plate (u, v)
HOLE_D = 6.4
HOLE_CSK_D = 8.4
HOLE_INSET_U = 7.5
HOLES = [(HOLE_INSET_U, L - 7.0), (W - HOLE_INSET_U, L - 7.0),
         (HOLE_INSET_U, 6.0)]

# --- mounting block (world coords) -----------------------------------------
BLK_X = 55.0          # block centre X
BLK_Y = 46.8          # Y of the front pair of holes
BLK_A = 13.3          # hole pattern: holes at (+-a, 0) and (0, a)
BLK_FR_CX = 14.3      # centre of the big front-corner arcs (+-cx, cy)
BLK_FR_CY = -3.0
BLK_FR_R = 9.6        # radius of the big front-corner arcs
BLK_FRONT = 9.5       # flat front face distance in front of the holes
BLK_R_FRONT = 2.0     # small fillet between front face and corner arcs
BLK_TOP_ABOVE = 1.2   # block top above the highest plate edge
BLK_HOLE_D = 9.0
BLK_HOLE_CSK = 11.0
BLK_HOLE_DEPTH = 15.0
BLK_TAP_D = 7.4       # smaller bore below the front holes (down to plate)
BLK_CH = 1.0

# --- boss near the front edge ----------------------------------------------
BOSS_X = 81.5
BOSS_Y = 6.9
BOSS_R = 7.7
BOSS_TOP = 15.5
BOSS_HOLE_D = 7.6
BOSS_HOLE_CSK = 9.4
BOSS_CH = 1.0

# --- horizontal lug at bottom-left -----------------------------------------
LUG_X = 17.3
LUG_Y = -5.8
LUG_R = 8.8           # radius of the round end
LUG_NECK = 7.2        # half width of the neck joining the plate
LUG_T = 7.0           # lug thickness (bottom flush with plate's lowest edge)
LUG_HOLE_D = 7.3
LUG_HOLE_CSK = 9.3
LUG_CH = 0.8

th = math.radians(THETA)
ct, st = math.cos(th), math.sin(th)


def to_world(shape):
    """Rotate a shape built in plate-local coords into the inclined pose."""
    return shape.rotate((0, 0, 0), (1, 0, 0), THETA)


def block_outline(wp):
    """Plan outline of the mounting block: two big front-corner arcs and a
    rear apex arc joined by 45 deg flanks, with a flat front face blended
    into the corner arcs by small fillets."""
    x0, y0 = BLK_X, BLK_Y
    cxr, cyr, R = BLK_FR_CX, BLK_FR_CY, BLK_FR_R
    s2 = math.sqrt(0.5)
    c45 = cxr + cyr + R * math.sqrt(2.0)       # flank line: |x| + y = c45
    ra = (c45 - BLK_A) / math.sqrt(2.0)        # apex radius (tangent)
    rf = BLK_R_FRONT
    yf = -BLK_FRONT
    # fillet centre between front line and right corner arc
    dyf = yf + rf - cyr
    dxf = math.sqrt((R - rf) ** 2 - dyf ** 2)
    fcx, fcy = cxr + dxf, yf + rf
    ux, uy = dxf / (R - rf), dyf / (R - rf)
    t_arc = (cxr + R * ux, cyr + R * uy)           # fillet / big arc
    bx, by = ux, uy - 1.0
    lb = math.hypot(bx, by)
    f_mid = (fcx + rf * bx / lb, fcy + rf * by / lb)
    a0 = math.atan2(uy, ux)
    a1 = math.radians(45.0)
    am = (a0 + a1) / 2
    arc_mid = (cxr + R * math.cos(am), cyr + R * math.sin(am))
    arc_end = (cxr + R * s2, cyr + R * s2)
    apex_r = (ra * s2, BLK_A + ra * s2)
    apex_m = (0.0, BLK_A + ra)

    def P(p, sx=1.0):
        return (x0 + sx * p[0], y0 + p[1])

    w = (
        wp.moveTo(*P((-fcx, yf)))
        .lineTo(*P((fcx, yf)))
        .threePointArc(P(f_mid), P(t_arc))
        .threePointArc(P(arc_mid), P(arc_end))
        .lineTo(*P(apex_r))
        .threePointArc(P(apex_m), P(apex_r, -1))
        .lineTo(*P(arc_end, -1))
        .threePointArc(P(arc_mid, -1), P(t_arc, -1))
        .threePointArc(P(f_mid, -1), P((fcx, yf), -1))
        .close()
    )
    return w


def csk_tool(x, y, z_top, d, d_csk, depth):
    """Vertical countersunk hole cutter starting at z_top going down."""
    bore = cq.Solid.makeCylinder(d / 2, depth + 1.0,
                                 cq.Vector(x, y, z_top + 1.0),
                                 cq.Vector(0, 0, -1))
    h = (d_csk - d) / 2
    cone = cq.Solid.makeCone(d_csk / 2 + 1.0, d / 2, h + 1.0,
                             cq.Vector(x, y, z_top + 1.0),
                             cq.Vector(0, 0, -1))
    return bore.fuse(cone)


# ---------------------------------------------------------------------------
# Plate outline
# ---------------------------------------------------------------------------
cx, cy = EAR_C
# lower (slanted) ear edge: tangent from the foot point to the ear circle
px, py = EAR_FOOT_U, 0.0
dx, dy = cx - px, cy - py
dist = math.hypot(dx, dy)
tang = math.atan2(dy, dx) - math.asin(EAR_R / dist)
tlen = math.sqrt(dist ** 2 - EAR_R ** 2)
Tpt = (px + tlen * math.cos(tang), py + tlen * math.sin(tang))
# upper ear edge: tangent from the neck point on the plate side
qx, qy = W, EAR_NECK_V
dx, dy = cx - qx, cy - qy
dist = math.hypot(dx, dy)
tang2 = math.atan2(dy, dx) + math.asin(EAR_R / dist)
tlen2 = math.sqrt(dist ** 2 - EAR_R ** 2)
Upt = (qx + tlen2 * math.cos(tang2), qy + tlen2 * math.sin(tang2))
a_t = math.atan2(Tpt[1] - cy, Tpt[0] - cx)
a_u = math.atan2(Upt[1] - cy, Upt[0] - cx)
a_mid = (a_t + a_u) / 2.0
ear_mid = (cx + EAR_R * math.cos(a_mid), cy + EAR_R * math.sin(a_mid))

rc = R_CORNER
k = 1 - math.sqrt(0.5)

outline = (
    cq.Workplane("XY", origin=(0, 0, -T))
    .moveTo(rc, 0)
    .lineTo(px, py)
    .lineTo(*Tpt)
    .threePointArc(ear_mid, Upt)
    .lineTo(qx, qy)
    .lineTo(W, L - rc)
    .threePointArc((W - rc * k, L - rc * k), (W - rc, L))
    .lineTo(rc, L)
    .threePointArc((rc * k, L - rc * k), (0, L - rc))
    .lineTo(0, rc)
    .threePointArc((rc * k, rc * k), (rc, 0))
    .close()
)
plate = outline.extrude(T)
# concave blend where the ear leaves the plate side
plate = plate.edges("|Z").edges(
    cq.selectors.BoxSelector((W - 0.1, EAR_NECK_V - 0.1, -T - 1),
                             (W + 0.1, EAR_NECK_V + 0.1, 1))
).fillet(EAR_FILLET)
plate = plate.faces(">Z or <Z").edges().chamfer(EDGE_CH)

# window
win = (
    cq.Workplane("XY", origin=(0, 0, -T - 1))
    .center((WIN_U[0] + WIN_U[1]) / 2, (WIN_V[0] + WIN_V[1]) / 2)
    .rect(WIN_U[1] - WIN_U[0], WIN_V[1] - WIN_V[0])
    .extrude(T + 2)
    .edges("|Z")
    .fillet(WIN_R)
)
plate = plate.cut(win)
plate = plate.faces(">Z").edges(
    cq.selectors.BoxSelector((WIN_U[0] - 1, WIN_V[0] - 1, -1),
                             (WIN_U[1] + 1, WIN_V[1] + 1, 1))
).chamfer(WIN_CH)

# countersunk mounting holes + plain ear hole (perpendicular to the plate)
for (hu, hv) in HOLES:
    plate = plate.cut(cq.Workplane().add(
        csk_tool(hu, hv, 0.0, HOLE_D, HOLE_CSK_D, T + 1.0)))
plate = plate.cut(
    cq.Workplane("XY", origin=(0, 0, -T - 1))
    .center(*EAR_C).circle(EAR_HOLE_D / 2).extrude(T + 2)
)

plate = to_world(plate)

# half-spaces used to trim the vertical features against the plate
BIG = 400.0
above_lower = to_world(
    cq.Workplane("XY").box(BIG, BIG, BIG, centered=(True, True, False))
    .translate((W / 2, L / 2, -T))
)
above_upper = to_world(
    cq.Workplane("XY").box(BIG, BIG, BIG, centered=(True, True, False))
    .translate((W / 2, L / 2, 0))
)
behind_front = to_world(
    cq.Workplane("XY").box(BIG, BIG, BIG, centered=(True, False, True))
    .translate((W / 2, 0, 0))
)
above_lower_inner = to_world(
    cq.Workplane("XY").box(BIG, BIG, BIG, centered=(True, False, False))
    .translate((W / 2, WIN_V[0] - 1.0, -T))
)

# ---------------------------------------------------------------------------
# Mounting block: rounded-triangle prism, trimmed by the plate underside
# ---------------------------------------------------------------------------
a = BLK_A
z_top = L * st + BLK_TOP_ABOVE
z_bot = 20.0
blk_outline = block_outline(cq.Workplane("XY", origin=(0, 0, z_bot)))
blk = blk_outline.extrude(z_top - z_bot)
blk = blk.faces(">Z").edges().chamfer(BLK_CH)
blk = blk.intersect(above_lower)
blk_holes = [(BLK_X - a, BLK_Y), (BLK_X + a, BLK_Y), (BLK_X, BLK_Y + a)]

# ---------------------------------------------------------------------------
# Boss near the front edge (vertical): sits on the upper face, stops at the
# front end plane, and fills the window corner it overhangs
# ---------------------------------------------------------------------------
boss = (
    cq.Workplane("XY", origin=(0, 0, -20))
    .circle(BOSS_R)
    .extrude(BOSS_TOP + 20)
    .rotate((0, 0, 0), (0, 0, 1), 90)
    .translate((BOSS_X, BOSS_Y, 0))
)
boss = boss.faces(">Z").edges().chamfer(BOSS_CH)
# above the plate the boss is cut by the (extended) upper face; where it
# overhangs the window it is carried down through the plate thickness
boss = boss.intersect(above_upper).intersect(behind_front).union(
    boss.intersect(above_lower_inner))

# ---------------------------------------------------------------------------
# Horizontal lug at the bottom-left
# ---------------------------------------------------------------------------
lug_z0 = -T * ct
lug_back = T * st - 0.5
yn = LUG_Y + math.sqrt(LUG_R ** 2 - LUG_NECK ** 2)   # neck meets the circle
lug = (
    cq.Workplane("XY", origin=(0, 0, lug_z0))
    .moveTo(LUG_X - LUG_NECK, lug_back)
    .lineTo(LUG_X - LUG_NECK, yn)
    .threePointArc((LUG_X, LUG_Y - LUG_R), (LUG_X + LUG_NECK, yn))
    .lineTo(LUG_X + LUG_NECK, lug_back)
    .close()
    .extrude(LUG_T)
)
lug = lug.faces(">Z or <Z").edges("not(>Y)").chamfer(LUG_CH)

# ---------------------------------------------------------------------------
# Combine, then drill the vertical holes through everything they meet
# ---------------------------------------------------------------------------
result = plate.union(blk).union(boss).union(lug)

for (hx, hy) in blk_holes:
    result = result.cut(cq.Workplane().add(
        csk_tool(hx, hy, z_top, BLK_HOLE_D, BLK_HOLE_CSK, BLK_HOLE_DEPTH)))


def bore_to_plate(x, y, d, z_from):
    """Vertical bore from z_from down to the plate's upper face."""
    cyl = cq.Workplane("XY", origin=(x, y, -40)).circle(d / 2).extrude(
        z_from + 40)
    return cyl.intersect(above_upper)


for (hx, hy) in blk_holes[:2]:
    result = result.cut(bore_to_plate(hx, hy, BLK_TAP_D,
                                      z_top - BLK_HOLE_DEPTH + 0.5))

boss_hole = cq.Workplane().add(
    csk_tool(BOSS_X, BOSS_Y, BOSS_TOP, BOSS_HOLE_D, BOSS_HOLE_CSK, 1.0)
).union(bore_to_plate(BOSS_X, BOSS_Y, BOSS_HOLE_D, BOSS_TOP))
result = result.cut(boss_hole)

result = result.cut(cq.Workplane().add(
    csk_tool(LUG_X, LUG_Y, lug_z0 + LUG_T, LUG_HOLE_D, LUG_HOLE_CSK,
             LUG_T + 2.0)))
